"""Bench clamp holder: a flat strap bent over at the top into a perforated
round pad, a second pad on a short arm lower down (the two pads face each
other with shallow dishes), and a C-clamp block at the foot with a jaw gap,
a pin between the jaws and a counterbored screw hole."""
import math
import cadquery as cq
from OCP.TopExp import TopExp
from OCP.TopTools import TopTools_IndexedDataMapOfShapeListOfShape
from OCP.TopAbs import TopAbs_EDGE, TopAbs_FACE

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
# pads (perforated disks)
DISK_R = 20.5           # pad radius
DISK_T = 11.0           # pad thickness
DISK_EDGE_R = 3.0       # pad rim rounding
RING_R = 14.7           # bolt circle of the 8 outer holes
HOLE_D = 5.8            # outer hole diameter
CENTER_HOLE_D = 6.6     # centre hole diameter
N_HOLES = 8
RECESS_D = 17.0         # shallow dish on the inner face of each pad
RECESS_DEPTH = 2.0
RECESS_RIM_R = 1.8

# plan-form of arms / clamp
NECK_HW = 10.8          # half width of the neck joining the pad
XR = 10.8               # common right face of neck, bar and clamp
ANG_C = 17.7            # left chamfer line  x + y = ANG_C
NECK_FILLET = 9.0       # concave round neck -> chamfer line

# vertical bar (flat strap)
BAR_Y0 = 39.0
BAR_Y1 = 47.0
BAR_X0 = -23.8

# heights
Z_TOP_ARM_B = 131.4     # underside of upper arm / upper pad
Z_TOP_ARM_T = 139.8     # top of upper arm
Z_LOW_ARM_B = 40.6      # underside of lower arm
Z_CLAMP_T = 51.0        # top of clamp = top of lower arm = top of lower pad
Z_GAP_T = 24.8          # jaw gap top
Z_GAP_B = 11.0          # jaw gap bottom

BEND_R_OUT = 4.5
BEND_R_IN = 2.8
ROOT_R = 4.2            # bar root fillets on the clamp

# clamp
CLAMP_Y0 = 32.4         # clamp front face
CLAMP_Y1 = 74.7         # clamp back face
CLAMP_XL = -42.3        # left-most extent of clamp
CORNER_BR = 10.8        # back-right plan radius (concentric with screw hole)
SPINE_XL = -19.2        # spine (material joining the jaws) left face
SPINE_YB = 42.8         # spine back face
PIN_D = 6.4             # pin joining the jaws
PIN_FILLET = 2.5
SCREW_D = 7.4
CBORE_D = 12.0
CBORE_DEPTH = 12.0
EDGE_R = 3.3            # general edge rounding
ARM_ROOT_R = 3.0        # lower arm underside into clamp front
GAP_INNER_R = 2.6
NECK_PAD_R = 2.0         # neck blends into the pad rim

# derived ------------------------------------------------------------------
S2 = math.sqrt(2.0)
CORNER_BL = (CLAMP_XL + CLAMP_Y1 - ANG_C) / S2
PIN_C = (CLAMP_XL + CORNER_BL, CLAMP_Y1 - CORNER_BL)
SCREW_C = (XR - CORNER_BR, CLAMP_Y1 - CORNER_BR)
NECK_Y = ANG_C + NECK_HW      # y where chamfer line meets neck left edge


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def edge_info(solid):
    """list of (edge, kind) with kind in convex / concave / smooth / other"""
    m = TopTools_IndexedDataMapOfShapeListOfShape()
    TopExp.MapShapesAndAncestors_s(solid.wrapped, TopAbs_EDGE, TopAbs_FACE, m)
    out = []
    for i in range(1, m.Extent() + 1):
        e = cq.Edge(m.FindKey(i))
        faces = [cq.Face(f) for f in m.FindFromIndex(i)]
        kind = "other"
        if len(faces) == 2:
            p = e.positionAt(0.5)
            n1 = faces[0].normalAt(p)
            n2 = faces[1].normalAt(p)
            if n1.dot(n2) > 0.995:
                kind = "smooth"
            else:
                d = n1 - n2
                a = solid.isInside(p + d * 0.05, 1e-4)
                b = solid.isInside(p - d * 0.05, 1e-4)
                kind = "convex" if (not a and not b) else (
                    "concave" if (a and b) else "other")
        out.append((e, kind))
    return out


FILLET_LOG = []


def fillet_where(solid, r, kind, pred):
    """round all edges of the given kind selected by pred; keep the solid
    unchanged if the kernel cannot build the blend"""
    es = [e for e, k in edge_info(solid)
          if k == kind and pred(e, e.BoundingBox())]
    if not es:
        FILLET_LOG.append((r, kind, 0, "none"))
        return solid
    try:
        res = solid.fillet(r, es)
        if res.isValid():
            FILLET_LOG.append((r, kind, len(es), "ok"))
            return res
    except Exception:
        pass
    FILLET_LOG.append((r, kind, len(es), "FAILED"))
    return solid


def near(a, b, tol=0.05):
    return abs(a - b) < tol


def neck_round():
    """points of the concave round between chamfer line and neck left edge"""
    r = NECK_FILLET
    cxn, cyn = -NECK_HW, NECK_Y
    t = r * math.tan(math.radians(22.5))
    p1 = (cxn - t / S2, cyn + t / S2)
    p2 = (cxn, cyn - t)
    cc = (cxn - r, cyn - t)
    a_mid = math.radians(22.5)
    pm = (cc[0] + r * math.cos(a_mid), cc[1] + r * math.sin(a_mid))
    return p1, pm, p2


def clamp_outline(y_front):
    """right face, rounded back corners, back face, left chamfer line"""
    cx, cy = PIN_C
    r = CORNER_BL
    t_line = (cx - r / S2, cy - r / S2)
    a = math.radians(157.5)
    mid_bl = (cx + r * math.cos(a), cy + r * math.sin(a))
    bx, by = SCREW_C
    rb = CORNER_BR
    mid_br = (bx + rb * math.cos(math.radians(45)),
              by + rb * math.sin(math.radians(45)))
    wp = cq.Workplane("XY").moveTo(XR, y_front)
    wp = wp.lineTo(XR, by)
    wp = wp.threePointArc(mid_br, (bx, CLAMP_Y1))
    wp = wp.lineTo(cx, CLAMP_Y1)
    wp = wp.threePointArc(mid_bl, t_line)
    return wp


def clamp_plan(y_front):
    return clamp_outline(y_front).lineTo(ANG_C - y_front, y_front).close()


def master_plan():
    """clamp plan-form continued forward as the neck to the pad centre"""
    p1, pm, p2 = neck_round()
    wp = clamp_outline(0.0).lineTo(*p1).threePointArc(pm, p2)
    return wp.lineTo(-NECK_HW, 0.0).close()


def strap_plan(y_back):
    """plan of the upper arm + bar: neck, chamfer line, bar width"""
    p1, pm, p2 = neck_round()
    yk = ANG_C - BAR_X0       # chamfer line meets bar left face
    return (cq.Workplane("XY").moveTo(XR, 0.0)
            .lineTo(XR, y_back)
            .lineTo(BAR_X0, y_back)
            .lineTo(BAR_X0, yk)
            .lineTo(*p1).threePointArc(pm, p2)
            .lineTo(-NECK_HW, 0.0)
            .close())


def strap_profile():
    """side (YZ) profile of upper arm bent down into the bar"""
    ri, ro = BEND_R_IN, BEND_R_OUT
    zb = Z_CLAMP_T - 4.0
    c = math.cos(math.radians(45))
    wp = (cq.Workplane("YZ").moveTo(0.0, Z_TOP_ARM_B)
          .lineTo(BAR_Y0 - ri, Z_TOP_ARM_B)
          .threePointArc((BAR_Y0 - ri + ri * c, Z_TOP_ARM_B - ri + ri * c),
                         (BAR_Y0, Z_TOP_ARM_B - ri))
          .lineTo(BAR_Y0, zb)
          .lineTo(BAR_Y1, zb)
          .lineTo(BAR_Y1, Z_TOP_ARM_T - ro)
          .threePointArc((BAR_Y1 - ro + ro * c, Z_TOP_ARM_T - ro + ro * c),
                         (BAR_Y1 - ro, Z_TOP_ARM_T))
          .lineTo(0.0, Z_TOP_ARM_T)
          .close())
    return wp


# ---------------------------------------------------------------------------
# clamp + lower arm
# ---------------------------------------------------------------------------
clamp = clamp_plan(CLAMP_Y0).extrude(Z_CLAMP_T)
low_arm = (master_plan().extrude(Z_CLAMP_T - Z_LOW_ARM_B)
           .translate((0, 0, Z_LOW_ARM_B)))
body = clamp.union(low_arm)

# jaw gap: everything outside the spine between the jaws
gap_h = Z_GAP_T - Z_GAP_B
g1 = cq.Workplane("XY").box(200, 200, gap_h, centered=(False, True, False)) \
    .translate((SPINE_XL - 200, 0, Z_GAP_B))
g2 = cq.Workplane("XY").box(200, 200, gap_h, centered=(True, False, False)) \
    .translate((0, SPINE_YB, Z_GAP_B))
body = body.cut(g1).cut(g2)

# ---------------------------------------------------------------------------
# strap: upper arm bent down into the vertical bar
# ---------------------------------------------------------------------------
# side profile (with both bend radii) extruded across the bar width, then
# trimmed to the plan-form of neck / chamfer / bar
prof = strap_profile()
strap = prof.extrude(XR - BAR_X0 + 2.0).translate((BAR_X0 - 1.0, 0, 0))
strap = strap.intersect(strap_plan(BAR_Y1 + 20.0).extrude(400)
                        .translate((0, 0, -10)))

body = body.union(strap)
B = body.val()

# inner rounds of the jaw gap
B = fillet_where(B, GAP_INNER_R, "concave",
                 lambda e, bb: bb.zmax < Z_GAP_T + 0.1 and bb.zmin > Z_GAP_B - 0.1)

# roots of the bar on the clamp (front, back and left side of the bar)
B = fillet_where(B, ROOT_R, "concave",
                 lambda e, bb: near(bb.zmin, Z_CLAMP_T) and near(bb.zmax, Z_CLAMP_T)
                 and (near(bb.ymin, BAR_Y0) and near(bb.ymax, BAR_Y0)
                      or near(bb.ymin, BAR_Y1) and near(bb.ymax, BAR_Y1)
                      or near(bb.xmin, BAR_X0) and near(bb.xmax, BAR_X0)))

# lower arm runs into the clamp front face with a small concave round
B = fillet_where(B, ARM_ROOT_R, "concave",
                 lambda e, bb: near(bb.zmin, Z_LOW_ARM_B) and near(bb.zmax, Z_LOW_ARM_B)
                 and near(bb.ymin, CLAMP_Y0) and near(bb.ymax, CLAMP_Y0))

# edge rounds on every remaining sharp outside edge (except the neck ends
# buried inside the pads); fall back to smaller radii if needed
for r_try in (EDGE_R, 0.8 * EDGE_R, 0.65 * EDGE_R):
    B = fillet_where(B, r_try, "convex", lambda e, bb: bb.ymax > 0.1)
    if FILLET_LOG[-1][3] != "FAILED":
        break

# ---------------------------------------------------------------------------
# pin joining the jaws (rounded into both jaws)
# ---------------------------------------------------------------------------
pin = cq.Workplane("XY").circle(PIN_D / 2).extrude(gap_h + 2.0) \
    .translate((PIN_C[0], PIN_C[1], Z_GAP_B - 1.0)).val()
B = B.fuse(pin).clean()
B = fillet_where(B, PIN_FILLET, "concave",
                 lambda e, bb: e.geomType() == "CIRCLE"
                 and abs((bb.xmin + bb.xmax) / 2 - PIN_C[0]) < 0.2
                 and abs((bb.ymin + bb.ymax) / 2 - PIN_C[1]) < 0.2)


# ---------------------------------------------------------------------------
# pads
# ---------------------------------------------------------------------------
def pad(z0):
    d = cq.Workplane("XY").circle(DISK_R).extrude(DISK_T).translate((0, 0, z0))
    return d.edges("%CIRCLE").fillet(DISK_EDGE_R).val()


B = B.fuse(pad(Z_TOP_ARM_B)).fuse(pad(Z_CLAMP_T - DISK_T)).clean()


def pad_junction(e, bb, zlo):
    """concave edges where a neck runs into a pad rim"""
    if bb.zmin < zlo - 0.1 or bb.zmax > zlo + DISK_T + 0.1:
        return False
    c = e.Center()
    return DISK_R - DISK_EDGE_R - 1.5 < math.hypot(c.x, c.y) < DISK_R + 0.5


for zlo in (Z_TOP_ARM_B, Z_CLAMP_T - DISK_T):
    B = fillet_where(B, NECK_PAD_R, "concave",
                     lambda e, bb, z=zlo: pad_junction(e, bb, z))

# shallow dished recess on the facing (inner) sides of the pads
for z_face, sgn in ((Z_TOP_ARM_B, 1.0), (Z_CLAMP_T, -1.0)):
    z0 = z_face if sgn > 0 else z_face - RECESS_DEPTH
    rc = cq.Workplane("XY").circle(RECESS_D / 2).extrude(RECESS_DEPTH) \
        .translate((0, 0, z0)).val()
    B = B.cut(rc).clean()
    B = fillet_where(B, RECESS_RIM_R, "convex",
                     lambda e, bb, z=z_face: e.geomType() == "CIRCLE"
                     and near(bb.zmin, z) and near(bb.zmax, z)
                     and near(bb.xmax - bb.xmin, RECESS_D, 0.1))

# holes through the pads
pts = [(RING_R * math.cos(2 * math.pi * i / N_HOLES),
        RING_R * math.sin(2 * math.pi * i / N_HOLES)) for i in range(N_HOLES)]
holes = cq.Workplane("XY").pushPoints(pts).circle(HOLE_D / 2).extrude(300) \
    .translate((0, 0, -50)).val()
B = B.cut(holes)
B = B.cut(cq.Workplane("XY").circle(CENTER_HOLE_D / 2).extrude(300)
          .translate((0, 0, -50)).val())

# clamp screw: through both jaws, counterbored from the top
B = B.cut(cq.Workplane("XY").circle(SCREW_D / 2).extrude(200)
          .translate((SCREW_C[0], SCREW_C[1], -50)).val())
B = B.cut(cq.Workplane("XY").circle(CBORE_D / 2).extrude(CBORE_DEPTH + 10)
          .translate((SCREW_C[0], SCREW_C[1], Z_CLAMP_T - CBORE_DEPTH)).val())

result = cq.Workplane("XY").add(B.clean())
